import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 59.0          # body width (X)
D = 34.5          # body depth (Y), front face at Y=0, back at Y=D
H = 39.5          # body height, top at Z=0, bottom at Z=-H
SIDE_STRAIGHT = H - W / 2.0   # vertical part of the side before the round bottom
R_FRONT = 9.25    # round on the front outline (vertical corners + bottom)
R_BACK = 8.6      # round on the back outline
Z_OH = -14.9      # underside of the front overhang
Y_LF = 16.4       # lower front face (set back)
XC = 22.4         # half width of the lower front recess

# pocket
RIM_F = 3.1
RIM_B = 2.9
TH_X = 19.1       # half width of through slot / pocket
TH_Y1 = RIM_F
TH_Y2 = 14.0
SLOT_X = 13.1     # half width of deep central slot
Z_FLOOR = -12.4   # floor of central slot
WELL_R = 8.9
WELL_X = 16.5
WELL_Y = 23.0
Z_PAD = -8.5      # floor of the end wells (pad top)
PAD_Y0 = 22.7     # where the pad front curve leaves the slot side wall
BOSS_X = 17.7
BOSS_R = 4.05
BOSS_HOLE_R = 2.5
BOSS_H = 2.4

# tube
TUBE_R = 12.2
BORE_R = 8.75
TUBE_ZC = -10.95
TUBE_LEN = 24.75  # protrusion in front of the body
BORE_DEPTH = 12.2 # blind bore depth from the tube front end

# legs (wishbone plate at the tube front end)
LEG_T = 10.0      # plate thickness (Y)
LEG_W = 4.7       # leg width
LEG_ANG = 30.0    # leg splay, deg from vertical
FOOT_X = 13.8     # foot centre offset from the tube axis (X)
FOOT_DZ = 24.2    # foot centre drop below the tube axis
WAIST_R = 8.0     # concave round between ring and outer leg edge
ARCH_R = 7.2      # round arch between the legs (touches the ring bottom)

# engraved star on the back face (8 rays, 45 deg apart, starting straight up, clockwise)
STAR_X = 0.0      # centred on the back face
STAR_Z = -12.9
STAR_W = 0.75
STAR_DEPTH = 0.5
STAR_DOT_R = 0.75
STAR_GAP = 1.6
STAR_RAYS = (8.5, 6.1, 8.4, 6.0, 14.8, 6.1, 8.4, 6.0)


def edges_of_face(solid, face_pred, edge_pred):
    out = []
    for f in solid.Faces():
        if face_pred(f):
            for e in f.Edges():
                if edge_pred(e):
                    out.append(e)
    return out


# ---------------- body ----------------
zc = -SIDE_STRAIGHT
R = W / 2.0
body = (
    cq.Workplane("XZ")
    .moveTo(-R, 0)
    .lineTo(R, 0)
    .lineTo(R, zc)
    .threePointArc((0, zc - R), (-R, zc))
    .close()
    .extrude(-D)          # XZ normal is -Y -> negative extrude goes to +Y
    .val()
)
fe = edges_of_face(
    body,
    lambda f: f.geomType() == "PLANE" and abs(f.Center().y) < 1e-6,
    lambda e: e.Center().z < -0.1,
)
body = body.fillet(R_FRONT, fe)
be = edges_of_face(
    body,
    lambda f: f.geomType() == "PLANE" and abs(f.Center().y - D) < 1e-6,
    lambda e: e.Center().z < -0.1,
)
body = body.fillet(R_BACK, be)
body = cq.Workplane("XY").add(body)

# central lower recess under the overhang
recess = (
    cq.Workplane("XY")
    .box(2 * XC, Y_LF + 5, H + 5, centered=(True, False, False))
    .translate((0, -5, Z_OH - H - 5))
)
body = body.cut(recess)

# ---------------- tube ----------------
tube = cq.Workplane("XZ", origin=(0, TH_Y1, TUBE_ZC)).circle(TUBE_R).extrude(TUBE_LEN + TH_Y1)
top_keep = cq.Workplane("XY").box(200, 200, 100, centered=(True, True, False)).translate((0, 0, -100))
tube = tube.intersect(top_keep)

# ---------------- legs (wishbone plate at the tube front end) ----------------
def wishbone(wp):
    """Closed outline of the ring + two splayed legs, with concave waist rounds
    and a round arch between the legs (coordinates X, Z on an XZ workplane)."""
    a = math.radians(LEG_ANG)
    h = LEG_W / 2.0
    R = TUBE_R
    sa, ca = math.sin(a), math.cos(a)
    F = (-FOOT_X, -FOOT_DZ)                 # left foot centre (relative to ring centre)
    u = (sa, ca)                            # up along the left leg
    n_out = (-ca, sa)                       # outward normal of the left leg
    outer0 = (F[0] + h * n_out[0], F[1] + h * n_out[1])
    inner0 = (F[0] - h * n_out[0], F[1] - h * n_out[1])
    foot_mid = (F[0] - h * u[0], F[1] - h * u[1])
    # arch: circle on the centre line tangent to both inner leg edges
    n_in = (ca, -sa)
    r = ARCH_R
    az = inner0[1] + ((-inner0[0]) * ca - r) / sa
    tA = (-r * n_in[0], az - r * n_in[1])
    arch_top = (0.0, az + r)
    # waist: circle tangent to the ring and to the outer leg edge
    rw = WAIST_R
    bx, bz = outer0[0] + rw * n_out[0], outer0[1] + rw * n_out[1]
    qb = 2 * (bx * sa + bz * ca)
    qc = bx * bx + bz * bz - (R + rw) ** 2
    t = (-qb - math.sqrt(qb * qb - 4 * qc)) / 2
    Cw = (bx + t * sa, bz + t * ca)
    tWl = (Cw[0] - rw * n_out[0], Cw[1] - rw * n_out[1])
    d = math.hypot(*Cw)
    tWr = (Cw[0] * R / d, Cw[1] * R / d)
    mx, mz = (tWr[0] + tWl[0]) / 2 - Cw[0], (tWr[1] + tWl[1]) / 2 - Cw[1]
    mm = math.hypot(mx, mz)
    waist_mid = (Cw[0] + rw * mx / mm, Cw[1] + rw * mz / mm)
    ang_r = math.atan2(tWr[1], tWr[0])
    if ang_r < 0:
        ang_r += 2 * math.pi
    ring_mid_ang = (math.pi / 2 + ang_r) / 2
    ring_mid = (R * math.cos(ring_mid_ang), R * math.sin(ring_mid_ang))

    def m(p):
        return (-p[0], p[1])

    def s(p):
        return (p[0], p[1] + TUBE_ZC)

    return (
        wp.moveTo(*s((0.0, R)))
        .threePointArc(s(ring_mid), s(tWr))
        .threePointArc(s(waist_mid), s(tWl))
        .lineTo(*s(outer0))
        .threePointArc(s(foot_mid), s(inner0))
        .lineTo(*s(tA))
        .threePointArc(s(arch_top), s(m(tA)))
        .lineTo(*s(m(inner0)))
        .threePointArc(s(m(foot_mid)), s(m(outer0)))
        .lineTo(*s(m(tWl)))
        .threePointArc(s(m(waist_mid)), s(m(tWr)))
        .threePointArc(s(m(ring_mid)), s((0.0, R)))
        .close()
    )


plate = wishbone(cq.Workplane("XZ", origin=(0, -TUBE_LEN, 0))).extrude(-LEG_T)
plate = plate.intersect(top_keep)

part = body.union(tube).union(plate)

# ---------------- pocket ----------------
# through slot (front part)
through = (
    cq.Workplane("XY")
    .box(2 * TH_X, TH_Y2 - TH_Y1, 60, centered=(True, False, False))
    .translate((0, TH_Y1, -59))
)
part = part.cut(through)

# wells down to pad level (trimmed at the inner back wall)
well_trim = (
    cq.Workplane("XY")
    .box(W, D - RIM_B, 30, centered=(True, False, False))
    .translate((0, 0, Z_PAD - 1))
)
for sx in (-1, 1):
    well = (
        cq.Workplane("XY").workplane(offset=Z_PAD)
        .center(sx * WELL_X, WELL_Y).circle(WELL_R).extrude(-Z_PAD + 1)
    ).intersect(well_trim)
    part = part.cut(well)

# rectangular pocket to pad level
pk = (
    cq.Workplane("XY")
    .box(2 * TH_X, D - RIM_B - TH_Y1, -Z_PAD + 1, centered=(True, False, False))
    .translate((0, TH_Y1, Z_PAD))
)
part = part.cut(pk)

# deep central slot between the pads; the pad fronts are circular arcs tangent to the
# slot side walls at Y=PAD_Y0 and running out at the back corners of the through slot
rho = (((TH_X - SLOT_X) ** 2) + (PAD_Y0 - TH_Y2) ** 2) / (2 * (TH_X - SLOT_X))
pc_x = SLOT_X + rho                     # arc centre (right side)
ang0 = math.pi
ang1 = math.atan2(TH_Y2 - PAD_Y0, TH_X - pc_x)
angm = (ang0 + ang1) / 2 if ang1 > 0 else (ang0 + ang1 + 2 * math.pi) / 2
mid_r = (pc_x + rho * math.cos(angm), PAD_Y0 + rho * math.sin(angm))
deep = (
    cq.Workplane("XY")
    .workplane(offset=Z_FLOOR)
    .moveTo(-SLOT_X, D - RIM_B)
    .lineTo(SLOT_X, D - RIM_B)
    .lineTo(SLOT_X, PAD_Y0)
    .threePointArc(mid_r, (TH_X, TH_Y2))
    .lineTo(-TH_X, TH_Y2)
    .threePointArc((-mid_r[0], mid_r[1]), (-SLOT_X, PAD_Y0))
    .close()
    .extrude(-Z_FLOOR + 1)
)
part = part.cut(deep)

# bosses with holes
for sx in (-1, 1):
    boss = (
        cq.Workplane("XY").workplane(offset=Z_PAD)
        .center(sx * BOSS_X, WELL_Y).circle(BOSS_R).extrude(BOSS_H)
    )
    part = part.union(boss)
    hole = (
        cq.Workplane("XY").workplane(offset=Z_PAD + BOSS_H)
        .center(sx * BOSS_X, WELL_Y).circle(BOSS_HOLE_R).extrude(-8)
    )
    part = part.cut(hole)

# blind bore in the tube
bore = (
    cq.Workplane("XZ", origin=(0, -TUBE_LEN - 1, TUBE_ZC))
    .circle(BORE_R)
    .extrude(-(BORE_DEPTH + 1))
)
part = part.cut(bore)

# engraved star on the back face
def groove(x0, z0, x1, z1):
    L = math.hypot(x1 - x0, z1 - z0)
    ang = math.degrees(math.atan2(z1 - z0, x1 - x0))
    return (
        cq.Workplane("XZ", origin=(0, D + 1, 0))
        .center((x0 + x1) / 2, (z0 + z1) / 2)
        .slot2D(L + STAR_W, STAR_W, ang)
        .extrude(1 + STAR_DEPTH)
    )

star = (
    cq.Workplane("XZ", origin=(0, D + 1, 0))
    .center(STAR_X, STAR_Z)
    .circle(STAR_DOT_R)
    .extrude(1 + STAR_DEPTH)
)
for k, L in enumerate(STAR_RAYS):
    t = math.radians(90 - 45 * k)
    x0 = STAR_X + STAR_GAP * math.cos(t)
    z0 = STAR_Z + STAR_GAP * math.sin(t)
    x1 = STAR_X + L * math.cos(t)
    z1 = STAR_Z + L * math.sin(t)
    star = star.union(groove(x0, z0, x1, z1))
part = part.cut(star)

result = part
